import math
import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge, BRepBuilderAPI_MakeFace, BRepBuilderAPI_Sewing
from OCP.GeomFill import GeomFill
from OCP.TopoDS import TopoDS
from OCP.Geom import Geom_TrimmedCurve
from OCP.GeomConvert import GeomConvert, GeomConvert_CompCurveToBSplineCurve
from OCP.TColStd import TColStd_Array1OfReal

# Thin sheet "scoop": a tapered U-shaped shell, ruled between a large round
# front rim (tilted plane) and a narrower back rim (near-vertical plane, with
# a shallow V at the bottom centre line), the two arm tops trimmed by a
# straight front flat and a concave arc.

# ---------------- driving dimensions (mm) ----------------
T = 1.5                 # sheet thickness
T_FWD = 0.4             # forward shift of the inner rim curves, as a fraction of T

# front rim: lies in a plane tilted back (bottom point further back)
F_BOT_Y = 28.0          # Y of the front rim at its lowest point (Z = 0)
F_TILT = 0.3017         # dY/dZ of the front rim plane (Y = F_BOT_Y - F_TILT*Z)
F_R = 67.6              # radius of the front rim (seen from the front)
F_END = 120.0           # construction: end angle of the lofted front arc (deg)

# back rim: nearly vertical plane; two arcs meeting in a shallow V at the bottom,
# each continued upward by a straight (vertical) tangent wall
B_Y0 = 54.2             # Y of back plane at Z = 0
B_TILT = 0.046          # dY/dZ (Y = B_Y0 - B_TILT*Z)
B_R = 59.6 + T          # radius of each back arc (outer skin, seen from the front)
B_OFF = 7.1             # sideways offset of the arc centres from the mid plane
B_CZ = 78.1             # centre height of the back arcs (start of straight wall)
B_TOP = 115.0           # construction: height reached by the straight back wall

RULING_SPANS = 10        # knot spans along the rulings (tessellation quality only)

# top edge profile of the two arms (in the YZ plane, cut through along X)
TOP_FRONT_Z = 92.35         # height of the front corner (on the front rim plane)
TOP_PEAK = (8.6, 97.9)      # end of the straight front flat
TOP_DIP = (25.8, 94.6)      # lowest point of the concave arc
TOP_BACK = (49.6, 100.0)    # back corner (on the back rim plane)


def plane_pt(y0, tilt, x, z):
    return cq.Vector(x, y0 - tilt * z, z)


def plane_arc(y0, tilt, cx, cz, r, a_start, a_end):
    """Arc (circle when seen from the front) lying in the plane Y = y0 - tilt*Z.
    Angles in degrees, measured in the XZ view from +X, counter-clockwise."""
    n = cq.Vector(0, -1.0, -tilt).normalized()
    centre = plane_pt(y0, tilt, cx, cz)
    rv = r * math.sqrt(1.0 + tilt * tilt)
    return cq.Edge.makeEllipse(r, rv, centre, n, cq.Vector(1, 0, 0), a_start, a_end, 1)


def edge_bspline(edge, u0, u1):
    """Edge geometry as a BSpline curve, affinely re-parameterised onto [u0, u1]."""
    crv = BRep_Tool.Curve_s(edge.wrapped, 0.0, 1.0)
    a, b = edge._bounds()
    bs = GeomConvert.CurveToBSplineCurve_s(Geom_TrimmedCurve(crv, a, b))
    n = bs.NbKnots()
    k0, k1 = bs.Knot(1), bs.Knot(n)
    ks = TColStd_Array1OfReal(1, n)
    for i in range(1, n + 1):
        ks.SetValue(i, u0 + (bs.Knot(i) - k0) * (u1 - u0) / (k1 - k0))
    bs.SetKnots(ks)
    return bs


def joined_curve(edges):
    """Chain of edges as one BSpline curve.  Piece i initially spans [i, i+1];
    at tangent joints the parameterisation is rescaled to stay C1, so that
    ruled surfaces built on these curves stay smooth."""
    comp = None
    for i, e in enumerate(edges):
        bs = edge_bspline(e, float(i), float(i + 1))
        if comp is None:
            comp = GeomConvert_CompCurveToBSplineCurve(bs)
        else:
            comp.Add(bs, 1e-6, True, True, 0)
    return comp.BSplineCurve()


def edge_from_curve(c):
    return cq.Edge(BRepBuilderAPI_MakeEdge(c).Edge())


def front_u(r, dy=0.0):
    """Front rim circle, centre on the mid plane; top-left -> bottom -> top-right.
    dy moves the curve's plane along Y (used for the inner skin)."""
    y0 = F_BOT_Y + dy
    return joined_curve([
        plane_arc(y0, F_TILT, 0.0, F_R, r, F_END, 180.0),
        plane_arc(y0, F_TILT, 0.0, F_R, r, 180.0, 270.0),
        plane_arc(y0, F_TILT, 0.0, F_R, r, 270.0, 360.0),
        plane_arc(y0, F_TILT, 0.0, F_R, r, 0.0, 180.0 - F_END),
    ])


def back_u(r, wall_x, dy=0.0):
    """Back rim: straight walls + two offset arcs meeting in a shallow V
    on the mid plane; top-left -> bottom -> top-right."""
    y0 = B_Y0 + dy
    a_bot = math.degrees(math.atan2(math.sqrt(r ** 2 - B_OFF ** 2), B_OFF))
    return joined_curve([
        cq.Edge.makeLine(plane_pt(y0, B_TILT, wall_x, B_TOP),
                         plane_pt(y0, B_TILT, wall_x, B_CZ)),
        plane_arc(y0, B_TILT, B_OFF, B_CZ, r, 180.0, 180.0 + a_bot),
        plane_arc(y0, B_TILT, -B_OFF, B_CZ, r, 360.0 - a_bot, 360.0),
        cq.Edge.makeLine(plane_pt(y0, B_TILT, -wall_x, B_CZ),
                         plane_pt(y0, B_TILT, -wall_x, B_TOP)),
    ])


def ruled_face(c_front, c_back):
    """Ruled face between two rim curves (matching parameters joined by straight
    lines).  Extra knots along the rulings change nothing in the geometry but
    give the face a finer, better shaped tessellation."""
    srf = GeomFill.Surface_s(c_front, c_back)
    u0, u1, v0, v1 = srf.Bounds()
    srf.IncreaseDegree(srf.UDegree(), 2)
    for k in range(1, RULING_SPANS):
        srf.InsertVKnot(v0 + (v1 - v0) * k / RULING_SPANS, 1, 1e-9, True)
    return cq.Face(BRepBuilderAPI_MakeFace(srf, 1e-7).Face())


b_wall = B_OFF - B_R    # X of the straight back wall (outer skin, left side)
# inner skin: rim curves shrunk by T and moved forward by T_FWD*T, so the rim
# faces sit roughly square to the sheet like a thickened (offset) surface
fo, fi = front_u(F_R), front_u(F_R - T, -T_FWD * T)                       # front rim
bo, bi = back_u(B_R, b_wall), back_u(B_R - T, b_wall + T, -T_FWD * T)     # back rim

outer = ruled_face(fo, bo)
inner = ruled_face(fi, bi)


def cap(c_out, c_in):
    """Rim face (thickness face) between the outer and inner U curves."""
    return cq.Face.makeRuledSurface(edge_from_curve(c_out), edge_from_curve(c_in))


def end_face(p_fo, p_fi, p_bo, p_bi):
    """Ruled face closing one (later trimmed away) end of the arm."""
    return cq.Face.makeRuledSurface(cq.Edge.makeLine(p_fo, p_fi), cq.Edge.makeLine(p_bo, p_bi))


def pt(c, u):
    p = c.Value(u)
    return cq.Vector(p.X(), p.Y(), p.Z())


ends = [
    end_face(pt(fo, par(fo)), pt(fi, par(fi)), pt(bo, par(bo)), pt(bi, par(bi)))
    for par in (lambda c: c.FirstParameter(), lambda c: c.LastParameter())
]

sew = BRepBuilderAPI_Sewing(1e-4)
for f in [outer, inner, cap(fo, fi), cap(bo, bi)] + ends:
    sew.Add(f.wrapped)
sew.Perform()
shell = cq.Shell(TopoDS.Shell_s(sew.SewedShape()))
sheet = cq.Solid.makeSolid(shell).fix()

# ---- top edge of the arms (profile in YZ, cut through along X)
fy0, fz0 = F_BOT_Y - F_TILT * TOP_FRONT_Z, TOP_FRONT_Z      # front corner
py, pz = TOP_PEAK
slope = (pz - fz0) / (py - fy0)
ext = 40.0
top_cut = (
    cq.Workplane("YZ", origin=(-200, 0, 0))
    .moveTo(fy0 - ext, fz0 - slope * ext)
    .lineTo(py, pz)
    .threePointArc(TOP_DIP, TOP_BACK)
    .lineTo(TOP_BACK[0] + 20.0, TOP_BACK[1] + 12.0)
    .lineTo(TOP_BACK[0] + 20.0, 250.0)
    .lineTo(fy0 - ext, 250.0)
    .close()
    .extrude(400)
)

result = cq.Workplane("XY").add(sheet).cut(top_cut)

VIEW = {"azimuth": 45, "elevation": 26}
